import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0            # plate side length (square)
CORNER_R = 2.5       # plate corner radius
T_BASE = 2.0         # base plate thickness
H_RAISE = 3.4        # height of raised rails / ribs / tabs above base top

STRIP_W = 13.9       # outer width of each arm strip
RAIL_W = 2.15        # rail (wall) width
POCKET_W = STRIP_W - 2 * RAIL_W
R_IN = 22.2          # inner radius of central ring (recess)
R_OUT = R_IN + RAIL_W
SLOT_W = 5.5         # width of the diagonal gaps in the ring rib
POCKET_END = L / 2 - 11.7   # pocket outer end distance from centre
POCKET_CR = 0.7      # pocket end corner radius
BASE_FILLET = 0.7    # concave fillet where raised walls meet the base top
NEG_Y_ARM_GAP = 4.4  # -Y arm strip stops this far short of the edge

ARM_HOLE_D = 3.1
ARM_HOLE_POS = L / 2 - 8.7
NUT_AF = 5.7         # hex nut trap (from below) across flats
NUT_DEPTH = 2.4

CORNER_HOLE_D = 4.7
CORNER_HOLE_INSET = 4.9

TAB_T = 2.2          # edge tab thickness
TAB_START = 11.1     # tab start distance from corner
TAB_LEN = 11.3       # tab length along edge

D_R = 13.9           # D-shaped cut-out radius
D_CX = 30.5          # D centre |x|
D_CY = -30.5         # D centre y
D_FLAT = -19.6       # y of flat side of D

NOTCH_DIST = 25.2    # notch outer edge distance from plate centre (on diagonal)
NOTCH_W = 13.3       # notch width
NOTCH_OFF = 1.4      # notch lateral offset from diagonal
NOTCH_DEPTH = 12.0
HOLE_CORNER_R = 0.6  # small radius on the cut-out corners

Z_TOP = T_BASE + H_RAISE

# ---------------- base plate ----------------
base = (
    cq.Workplane("XY")
    .rect(L, L)
    .extrude(T_BASE)
    .edges("|Z")
    .fillet(CORNER_R)
)

# ---------------- raised layer ----------------
def raised_box(x0, x1, y0, y1):
    return (
        cq.Workplane("XY")
        .workplane(offset=T_BASE)
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .rect(x1 - x0, y1 - y0)
        .extrude(H_RAISE)
    )

hw = STRIP_W / 2
raised = (
    cq.Workplane("XY").workplane(offset=T_BASE).circle(R_OUT).extrude(H_RAISE)
)
raised = raised.union(raised_box(-hw, hw, 0, L / 2))                     # +Y arm
raised = raised.union(raised_box(-hw, hw, -L / 2 + NEG_Y_ARM_GAP, 0))    # -Y arm
raised = raised.union(raised_box(0, L / 2, -hw, hw))                     # +X arm
raised = raised.union(raised_box(-L / 2, 0, -hw, hw))                    # -X arm

# central recess
cutter = cq.Workplane("XY").workplane(offset=T_BASE).circle(R_IN).extrude(H_RAISE + 1)

# arm pockets (rounded outer corners)
for ang in (0, 90, 180, 270):
    pk = (
        cq.Workplane("XY")
        .workplane(offset=T_BASE)
        .sketch()
        .push([(POCKET_END / 2, 0)])
        .rect(POCKET_END, POCKET_W)
        .reset()
        .vertices(">X")
        .fillet(POCKET_CR)
        .finalize()
        .extrude(H_RAISE + 1)
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    cutter = cutter.union(pk)

# diagonal gaps in the ring rib
for ang in (45, 135, 225, 315):
    sl = (
        cq.Workplane("XY")
        .workplane(offset=T_BASE)
        .center((R_IN + R_OUT) / 2, 0)
        .rect(2 * (R_OUT - R_IN) + 4, SLOT_W)
        .extrude(H_RAISE + 1)
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    cutter = cutter.union(sl)

raised = raised.cut(cutter)

# edge tabs (on -X, +Y and +X edges, near both corners)
a0 = -L / 2 + TAB_START
a1 = a0 + TAB_LEN
b0 = L / 2 - TAB_START - TAB_LEN
b1 = L / 2 - TAB_START
tabs = [
    (-L / 2, -L / 2 + TAB_T, a0, a1), (-L / 2, -L / 2 + TAB_T, b0, b1),   # -X edge
    (L / 2 - TAB_T, L / 2, a0, a1), (L / 2 - TAB_T, L / 2, b0, b1),       # +X edge
    (a0, a1, L / 2 - TAB_T, L / 2), (b0, b1, L / 2 - TAB_T, L / 2),       # +Y edge
]
for (x0, x1, y0, y1) in tabs:
    raised = raised.union(raised_box(x0, x1, y0, y1))

part = base.union(raised)

# concave fillet along the foot of every raised wall
def _foot_edge(e):
    bb = e.BoundingBox()
    if abs(bb.zmin - T_BASE) > 1e-4 or abs(bb.zmax - T_BASE) > 1e-4:
        return False
    c = e.Center()
    lim = L / 2 - 1e-3
    # exclude the plate outline (convex) edges
    if abs(c.x) >= lim or abs(c.y) >= lim:
        return False
    if abs(c.x) > L / 2 - CORNER_R - 1e-3 and abs(c.y) > L / 2 - CORNER_R - 1e-3:
        return False
    return True

foot = [e for e in part.val().Edges() if _foot_edge(e)]
part = cq.Workplane("XY").newObject([part.val().fillet(BASE_FILLET, foot)])

# ---------------- holes ----------------
ci = L / 2 - CORNER_HOLE_INSET
part = (
    part.faces("<Z").workplane(centerOption="CenterOfBoundBox")
    .pushPoints([(ci, ci), (-ci, ci), (ci, -ci), (-ci, -ci)])
    .hole(CORNER_HOLE_D)
)

arm_pts = [(ARM_HOLE_POS, 0), (-ARM_HOLE_POS, 0), (0, ARM_HOLE_POS), (0, -ARM_HOLE_POS)]
hole_cut = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints(arm_pts).circle(ARM_HOLE_D / 2).extrude(Z_TOP + 2)
)
nut_cut = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints(arm_pts).polygon(6, NUT_AF / math.cos(math.radians(30))).extrude(NUT_DEPTH + 1)
)
part = part.cut(hole_cut).cut(nut_cut)

# ---------------- D-shaped cut-outs ----------------
def d_cut(cx):
    # semicircle (lower half) + rectangle up to the flat side
    return (
        cq.Workplane("XY").workplane(offset=-1)
        .moveTo(cx - D_R, D_FLAT)
        .lineTo(cx + D_R, D_FLAT)
        .lineTo(cx + D_R, D_CY)
        .threePointArc((cx, D_CY - D_R), (cx - D_R, D_CY))
        .close()
        .extrude(Z_TOP + 2)
    )

part = part.cut(d_cut(-D_CX)).cut(d_cut(D_CX))

# key notch on the +X/-Y cut-out, pointing to the plate centre
u = (1 / math.sqrt(2), -1 / math.sqrt(2))   # diagonal direction
v = (1 / math.sqrt(2), 1 / math.sqrt(2))    # lateral direction
nc = NOTCH_DIST + NOTCH_DEPTH / 2
ncx = u[0] * nc + v[0] * NOTCH_OFF
ncy = u[1] * nc + v[1] * NOTCH_OFF
notch = (
    cq.Workplane("XY").workplane(offset=-1)
    .center(ncx, ncy)
    .rect(NOTCH_DEPTH, NOTCH_W)
    .extrude(Z_TOP + 2)
    .rotate((ncx, ncy, 0), (ncx, ncy, 1), -45)
)
part = part.cut(notch)

# round the sharp (convex-in-hole) corners of the cut-outs
nA = (u[0] * NOTCH_DIST - v[0] * (NOTCH_W / 2 - NOTCH_OFF), u[1] * NOTCH_DIST - v[1] * (NOTCH_W / 2 - NOTCH_OFF))
nB = (u[0] * NOTCH_DIST + v[0] * (NOTCH_W / 2 + NOTCH_OFF), u[1] * NOTCH_DIST + v[1] * (NOTCH_W / 2 + NOTCH_OFF))
corner_pts = [(-D_CX - D_R, D_FLAT), (-D_CX + D_R, D_FLAT), (D_CX + D_R, D_FLAT), nA, nB]

def _is_corner_edge(e):
    bb = e.BoundingBox()
    if bb.xlen > 1e-3 or bb.ylen > 1e-3 or bb.zlen < 1e-3:
        return False
    return any(abs(bb.xmin - px) < 1e-2 and abs(bb.ymin - py) < 1e-2 for (px, py) in corner_pts)

corner_edges = [e for e in part.val().Edges() if _is_corner_edge(e)]
part = cq.Workplane("XY").newObject([part.val().fillet(HOLE_CORNER_R, corner_edges)])

result = part

VIEW = {"azimuth": 45, "elevation": 26}
